import math
import cadquery as cq
from OCP.gp import gp_GTrsf, gp_Mat, gp_XYZ
from OCP.BRepBuilderAPI import BRepBuilderAPI_GTransform
from OCP.BRepOffsetAPI import BRepOffsetAPI_ThruSections

# ---------------------------------------------------------------------------
# Winged gargoyle holding a mace.
# X = figure's left, the figure faces -Y, Z up, feet standing on Z = 0.
# ---------------------------------------------------------------------------

BX = -2.3                      # body centre line (X)

# torso ellipsoids: (centre, radii)
CHEST = ((BX, 0.5, 59.0), (16.0, 10.5, 10.0))
BELLY = ((BX, -2.0, 47.5), (13.0, 11.0, 10.0))
WAIST = ((BX, -0.5, 39.0), (12.5, 10.0, 6.0))
UPPER_BACK = ((BX, 5.0, 63.0), (13.0, 7.0, 8.0))
BELT = dict(z0=37.0, h=6.0, yc=-2.0, rx=14.0, ry=11.8, tilt=8.0)   # tilt: front dips (deg about X)

# head
HEAD_X = 1.5
CRANIUM = ((HEAD_X, -1.8, 77.5), (6.0, 6.5, 6.0))
MUZZLE = ((HEAD_X, -8.3, 75.3), (4.5, 5.3, 3.2))
JAW = ((HEAD_X, -6.5, 70.8), (4.1, 5.3, 2.4))
BROW = ((HEAD_X, -6.8, 79.6), (5.8, 2.5, 1.9))
NECK = ((BX + 1.5, 1.0, 69.5), (10.5, 7.5, 5.0))
# ram-like horns arching from the back of the skull forward (given for the +X side, mirrored)
HORN = [(3.2, 2.0, 80.8), (6.8, 0.5, 84.0), (8.2, -5.5, 84.0), (7.2, -12.0, 79.8)]
HORN_R = [2.1, 1.8, 1.3, 0.35]

# arms: shoulder, elbow, fist centre
R_SHOULDER, R_ELBOW, R_FIST = (-20.5, 1.5, 63.5), (-32.0, 3.5, 53.0), (-30.5, -5.0, 44.5)
L_SHOULDER, L_ELBOW, L_FIST = (16.0, 1.5, 64.0), (23.5, 6.5, 51.0), (26.5, -1.5, 40.5)
DELTOID_R, UPPER_ARM_R, FOREARM_R, FIST_R = 5.9, 4.8, 5.2, 4.7

# mace
MACE_HEAD_C = (-30.3, -25.0, 39.0)
MACE_HEAD_LEN, MACE_HEAD_RAD = 13.0, 5.0
MACE_SHAFT_R = 1.4

# legs: hip, knee, ankle, foot centre, foot radii
LEGS = [((-9.5, 1.0, 32.0), (-19.0, -6.0, 19.0), (-21.5, 1.0, 7.5), (-21.5, -2.5, 3.4), (6.3, 9.0, 4.4)),
        ((5.5, 1.0, 32.0), (19.0, -6.0, 19.0), (22.0, 1.5, 7.5), (22.5, -2.0, 3.4), (6.6, 9.5, 4.4))]
THIGH_R, KNEE_R, ANKLE_R = 6.8, 5.4, 4.0

# loin cloth
SKIRT = [(16.5, 0.0, 18.0, 12.2), (38.0, -1.0, 13.5, 10.5)]     # (z, y-centre, rx, ry)
CLOTH_Y, CLOTH_T = -13.0, 1.8

# tail: centre line, (half width in X, half height in Z)
TAIL_PTS = [(0.0, 8.0, 43.0), (2.0, 16.0, 35.5), (2.0, 24.0, 29.0), (-2.0, 31.0, 23.0), (-10.5, 37.5, 16.5)]
TAIL_RAD = [(3.0, 6.5), (2.6, 5.0), (2.1, 3.6), (1.5, 2.4), (0.5, 0.6)]

# wings.  W wrist, P* leading spar, T tip, R* trailing edge, L lowest trailing point,
# F* fold line, E* inner trailing edge, I inner root, S shoulder root, K inner back fold, C* claw
WING_R = dict(W=(-17.0, 11.0, 92.5), P1=(-33.0, 9.5, 95.5), P2=(-47.5, 9.5, 96.3), P3=(-68.0, 10.0, 94.0),
              P4=(-86.7, 10.5, 86.3), T=(-99.3, 11.0, 78.0),
              R1=(-88.0, 16.0, 76.5), R2=(-75.7, 19.5, 66.0), R3=(-64.7, 19.5, 53.3), L=(-55.4, 19.5, 37.6),
              F1=(-33.4, 14.0, 77.0), F2=(-44.4, 16.5, 67.5), F3=(-50.7, 18.0, 55.0),
              E1=(-39.7, 19.0, 41.6), E2=(-28.0, 16.0, 45.0), I=(-15.0, 12.0, 50.0), S=(-13.0, 11.0, 62.0),
              K=(-27.0, 27.0, 66.0),
              C1=(-13.8, 10.0, 96.2), C2=(-5.5, 8.0, 95.0))
WING_L = dict(W=(12.0, 9.0, 92.5), P1=(30.0, 15.5, 97.9), P2=(47.4, 20.0, 98.6), P3=(66.2, 24.5, 94.7),
              P4=(83.0, 29.0, 88.6), T=(93.0, 31.0, 84.6),
              R1=(81.0, 36.5, 80.7), R2=(70.9, 32.5, 67.4), R3=(61.5, 28.0, 54.9), L=(53.6, 23.5, 41.5),
              F1=(31.7, 17.0, 78.4), F2=(42.7, 20.0, 69.0), F3=(48.9, 22.0, 58.0),
              E1=(42.7, 20.0, 43.9), E2=(31.7, 16.0, 47.0), I=(12.0, 12.0, 50.0), S=(9.0, 11.0, 62.0),
              K=(25.6, 30.0, 66.0),
              C1=(9.5, 8.5, 96.2), C2=(1.0, 6.0, 94.5))
MEMBRANE_T = 1.3
SPAR_R = 1.2             # leading-edge bone radius
MEMBRANE_DIR = (0.0, 1.0, 0.0)   # membrane sheets are thickened along Y
WING_ARM_R = 2.6
ARM_INSET = 1.2         # membrane anchor offset from the wing-arm axis
JOINT_BULGE = 1.08       # joint spheres slightly proud of the limb cones


# ---------------------------------------------------------------------------
# helpers
# ---------------------------------------------------------------------------
def V(p):
    return cq.Vector(*p)


def ellipsoid(c, r):
    sph = cq.Solid.makeSphere(1.0, angleDegrees1=-90, angleDegrees2=90)
    g = gp_GTrsf()
    g.SetVectorialPart(gp_Mat(r[0], 0, 0, 0, r[1], 0, 0, 0, r[2]))
    g.SetTranslationPart(gp_XYZ(*c))
    return cq.Shape.cast(BRepBuilderAPI_GTransform(sph.wrapped, g, True).Shape())


def sphere(c, r):
    return cq.Solid.makeSphere(r, pnt=V(c), angleDegrees1=-90, angleDegrees2=90)


def cone(p1, p2, r1, r2):
    a, b = V(p1), V(p2)
    d = b - a
    if abs(r1 - r2) < 1e-6:
        return cq.Solid.makeCylinder(r1, d.Length, a, d.normalized())
    return cq.Solid.makeCone(r1, r2, d.Length, a, d.normalized())


def chain(pts, radii, end_caps=(True, True)):
    """Tapered tube through points: cones with spheres at the joints."""
    out = []
    for i in range(len(pts) - 1):
        out.append(cone(pts[i], pts[i + 1], radii[i], radii[i + 1]))
    for i in range(1, len(pts) - 1):
        out.append(sphere(pts[i], radii[i] * JOINT_BULGE))
    if end_caps[0]:
        out.append(sphere(pts[0], radii[0] * JOINT_BULGE))
    if end_caps[1] and radii[-1] > 0.3:
        out.append(sphere(pts[-1], radii[-1] * JOINT_BULGE))
    return out


def ellipse_loft(sections):
    """sections: list of (centre, normal, xdir, rx, ry) -> smooth lofted solid."""
    wires = [cq.Wire.makeEllipse(rx, ry, V(c), V(n), V(xd)) for (c, n, xd, rx, ry) in sections]
    return cq.Solid.makeLoft(wires)


def horizontal_loft(secs, x0=0.0):
    return ellipse_loft([((x0, yc, z), (0, 0, 1), (1, 0, 0), rx, ry) for (z, yc, rx, ry) in secs])


def tube_loft(pts, rads, side=(1.0, 0.0, 0.0)):
    """Loft of ellipses along a centre polyline; rads = (r along 'side', r across)."""
    secs = []
    n = len(pts)
    for i in range(n):
        a = V(pts[max(i - 1, 0)])
        b = V(pts[min(i + 1, n - 1)])
        t = (b - a).normalized()
        s = V(side)
        s = (s - t * s.dot(t)).normalized()
        secs.append((pts[i], t.toTuple(), s.toTuple(), rads[i][0], rads[i][1]))
    # makeEllipse needs major >= minor along xdir; swap axes when needed
    fixed = []
    for (c, t, s, r_side, r_up) in secs:
        if r_side >= r_up:
            fixed.append((c, t, s, r_side, r_up))
        else:
            up = V(t).cross(V(s)).normalized()
            fixed.append((c, t, up.toTuple(), r_up, r_side))
    return ellipse_loft(fixed)


def spline(pts):
    return cq.Edge.makeSpline([V(p) for p in pts])


def lerp(a, b, f):
    return tuple(a[i] * (1.0 - f) + b[i] * f for i in range(3))


def ruled_sheet(chain_a, chain_b, direction, t):
    """Smooth ruled surface between two splines, given thickness by a short extrusion."""
    f = cq.Face.makeRuledSurface(spline(chain_a), spline(chain_b))
    dv = V(direction).normalized()
    return cq.Solid.extrudeLinear(f.translate(dv * (-t / 2.0)), dv * t)


def loft_sheet(curves, direction, t):
    """Smooth sheet lofted through a few open spline curves, given thickness by extrusion."""
    ts = BRepOffsetAPI_ThruSections(False, False)
    for c in curves:
        ts.AddWire(cq.Wire.assembleEdges([spline(c)]).wrapped)
    ts.Build()
    f = cq.Shape.cast(ts.Shape()).Faces()[0]
    dv = V(direction).normalized()
    return cq.Solid.extrudeLinear(f.translate(dv * (-t / 2.0)), dv * t)


def wing_membrane(w, normal):
    """Bat-wing membrane from three smooth sheets:
       A   ruled: leading spar (wrist..P2)  -> fold line (wrist..L)
       B   ruled: leading spar (P2..tip)    -> trailing edge (L..tip)
       CD  lofted: fold line -> inner back ridge (arm..K..E1) -> body attachment (S..I..E2)
    The arm-side anchors sit a little off the wing-arm axis (inside the bone) and the inner
    sheet starts just inside sheet A, so every sheet meets its neighbours transversally."""
    o = ARM_INSET * (1.0 if w["T"][0] > 0 else -1.0)

    def inset(p):
        return (p[0] + o, p[1], p[2])

    w_top = inset(w["W"])
    w_fold = inset(lerp(w["W"], w["S"], 0.12))
    w_ridge = inset(lerp(w["W"], w["S"], 0.30))
    s_root = inset(w["S"])
    tip_in = lerp(w["T"], w["R1"], 0.04)
    t = MEMBRANE_T
    fold_in = [lerp(w_fold, w_top, 0.1), lerp(w["F1"], w["P1"], 0.04), lerp(w["F2"], w["P2"], 0.03),
               lerp(w["F3"], w["P2"], 0.03), lerp(w["L"], w["P2"], 0.015)]
    return [
        ruled_sheet([w_top, w["P1"], w["P2"]], [w_fold, w["F1"], w["F2"], w["F3"], w["L"]], normal, t),
        ruled_sheet([lerp(w["P2"], w["P1"], 0.08), w["P3"], w["P4"], w["T"]],
                    [lerp(w["L"], w["F3"], 0.08), w["R3"], w["R2"], w["R1"], tip_in], normal, t),
        loft_sheet([fold_in, [w_ridge, w["K"], w["E1"]], [s_root, w["I"], w["E2"]]], normal, t),
    ]


def box(c, size):
    return cq.Solid.makeBox(size[0], size[1], size[2],
                            V((c[0] - size[0] / 2, c[1] - size[1] / 2, c[2] - size[2] / 2)))


# ---------------------------------------------------------------------------
# build
# ---------------------------------------------------------------------------

def fuse(shapes):
    return shapes[0].fuse(*shapes[1:]) if len(shapes) > 1 else shapes[0]


groups = []

# ---- torso, belt, skirt ----
torso = [ellipsoid(*CHEST), ellipsoid(*BELLY), ellipsoid(*WAIST), ellipsoid(*UPPER_BACK), ellipsoid(*NECK)]
belt_c = V((BX, BELT["yc"], BELT["z0"] + BELT["h"] / 2.0))
belt = [cq.Workplane("XY").workplane(offset=BELT["z0"]).center(BX, BELT["yc"])
        .ellipse(BELT["rx"], BELT["ry"]).extrude(BELT["h"]).val(),
        box((BX - 5.0, BELT["yc"] - BELT["ry"] - 0.8, BELT["z0"] + 2.0), (7.0, 3.5, 8.0)),    # pouch
        box((BX + 3.5, BELT["yc"] - BELT["ry"] - 0.3, BELT["z0"] + 3.0), (5.0, 2.0, 5.0))]    # buckle
torso += [b.rotate(belt_c, belt_c + V((1, 0, 0)), BELT["tilt"]) for b in belt]
torso.append(horizontal_loft(SKIRT, BX))
torso.append(cq.Workplane("XZ", origin=(0, CLOTH_Y + CLOTH_T, 0))
             .polyline([(-7.5, 40.0), (9.5, 40.0), (8.5, 12.5), (5.0, 14.5), (2.0, 10.5), (-1.5, 13.5),
                        (-4.5, 11.5), (-7.0, 14.0)]).close().extrude(CLOTH_T).val())
groups.append(fuse(torso))

# ---- head ----
hd = [ellipsoid(*CRANIUM), ellipsoid(*MUZZLE), ellipsoid(*JAW), ellipsoid(*BROW)]
for s in (-1, 1):
    hd += chain([(HEAD_X + s * p[0], p[1], p[2]) for p in HORN], HORN_R, end_caps=(False, False))
for s in (-1, 1):
    hd.append(cone((HEAD_X + s * 4.8, 0.5, 78.0), (HEAD_X + s * 10.5, 2.5, 80.5), 1.6, 0.3))     # ears
    hd.append(cone((HEAD_X + s * 2.2, -11.5, 73.5), (HEAD_X + s * 2.4, -12.0, 71.0), 0.8, 0.2))  # fangs
groups.append(fuse(hd))

# ---- arms ----
for sh, el, fi, is_mace in ((R_SHOULDER, R_ELBOW, R_FIST, True), (L_SHOULDER, L_ELBOW, L_FIST, False)):
    arm = [sphere(sh, DELTOID_R),
           cone(sh, el, UPPER_ARM_R + 0.6, UPPER_ARM_R),
           sphere(el, UPPER_ARM_R * JOINT_BULGE),
           cone(el, fi, FOREARM_R, FIST_R - 0.8),
           ellipsoid(fi, (FIST_R, FIST_R + 0.3, FIST_R + 0.4))]
    if is_mace:
        # bracer
        mid = tuple(el[i] * 0.35 + fi[i] * 0.65 for i in range(3))
        arm.append(cone(el, mid, FOREARM_R + 0.8, FOREARM_R + 0.4))
        # mace: shaft from the fist forward to a spiked head
        mh, f0 = V(MACE_HEAD_C), V(fi)
        axis = (mh - f0).normalized()
        arm.append(cone(fi, (mh - axis * 1.0).toTuple(), MACE_SHAFT_R, MACE_SHAFT_R))
        h0 = mh - axis * (MACE_HEAD_LEN / 2.0)                    # collar end of the head
        h1 = mh + axis * (MACE_HEAD_LEN / 2.0 - MACE_HEAD_RAD)      # centre of the rounded far end
        arm.append(cq.Solid.makeCylinder(MACE_HEAD_RAD, (h1 - h0).Length, h0, axis))
        arm.append(sphere(h1.toTuple(), MACE_HEAD_RAD * JOINT_BULGE))
        arm.append(cq.Solid.makeCylinder(MACE_HEAD_RAD + 0.9, 2.2, h0 - axis * 0.4, axis))   # collar
        side = V((1, 0, 0))
        upv = axis.cross(side).normalized()
        for k in range(5):
            a = 2 * math.pi * (k + 0.25) / 5
            d = side * math.cos(a) + upv * math.sin(a)
            base = h0 + axis * 0.7
            arm.append(cone((base + d * 3.0).toTuple(), (base + d * (MACE_HEAD_RAD + 3.6) - axis * 0.8).toTuple(),
                            1.2, 0.2))
    else:
        for k in (-1, 0, 1):                                      # claws of the free hand
            base = (fi[0] + k * 2.2, fi[1] - 3.0, fi[2] - 2.5)
            arm.append(cone(base, (base[0] + k * 0.5, base[1] - 2.0, base[2] - 3.5), 1.0, 0.2))
    groups.append(fuse(arm))

# ---- legs ----
for hip, knee, ankle, foot, frad in LEGS:
    leg = chain([hip, knee, ankle], [THIGH_R, KNEE_R, ANKLE_R], end_caps=(False, False))
    leg.append(ellipsoid(foot, frad))
    for k in (-1, 0, 1):                                          # toe claws
        base = (foot[0] + k * 3.2, foot[1] - frad[1] + 2.0, foot[2])
        leg.append(cone(base, (base[0] + k * 0.8, base[1] - 3.5, 0.6), 1.6, 0.3))
    groups.append(fuse(leg))

# ---- tail ----
tl = [tube_loft(TAIL_PTS, TAIL_RAD)]
for i, (y, z) in enumerate(((13.0, 40.5), (19.0, 35.0), (25.0, 30.0))):
    x = 1.0 if i < 2 else 0.5
    tl.append(cone((x, y, z - 1.0), (x, y + 4.0, z + 2.5), 1.6, 0.2))
groups.append(fuse(tl))

# ---- wings ----
for w in (WING_R, WING_L):
    wg = wing_membrane(w, MEMBRANE_DIR)
    # leading-edge bone: a round spar swept along the spar curve
    spar = spline([w["W"], w["P1"], w["P2"], w["P3"], w["P4"], lerp(w["P4"], w["T"], 0.75)])
    ring = cq.Wire.assembleEdges([cq.Edge.makeCircle(SPAR_R, spar.startPoint(), spar.tangentAt(0))])
    wg.append(cq.Solid.sweep(ring, [], cq.Wire.assembleEdges([spar])))
    # wing arm rising behind the shoulder to the hooked thumb claw
    wg += chain([w["S"], w["W"], w["C1"], w["C2"]], [WING_ARM_R + 0.8, WING_ARM_R, 2.4, 0.5],
                end_caps=(True, False))
    groups.append(fuse(wg))

body = fuse(groups).clean()
body = body.cut(cq.Solid.makeBox(400, 400, 50, V((-200, -200, -50))))       # flat soles

result = cq.Workplane("XY").add(body)
VIEW = {"azimuth": 45, "elevation": 26}
